import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_O = 50.0          # outer radius over tread lugs
R_C = 46.2          # carcass (tread base) radius
R_BORE = 22.2       # bead inner radius (opening of the tire)
R_BEAD_FLAT = 24.45 # flat bead top ring R_BORE..R_BEAD_FLAT (sharp outer edge)
Z_BEAD = 18.2       # bead top height
LIP_MID = (24.9, 19.15)  # mid point of the rounded lip from the sidewall down to the bead ring
SIDE_IN = 25.6      # sidewall arc inner end
Z_BEAD_IN = 12.8    # underside of the bead (inside the tire)
R_BEAD_IN = 24.4    # bead inner face is undercut: R_BORE at the top, this at the bottom
WALL = 3.0          # tread wall thickness (hollow tire)
CEIL_Z = 17.0       # flat ceiling of the air cavity (thick sidewalls)
BEAD_OUT_R = 26.0   # bead ring bottom spans R_BEAD_IN..BEAD_OUT_R
CAV_CORNER = 1.5    # round between cavity ceiling and inner tread
BEAD_FILLET = CEIL_Z - Z_BEAD_IN  # fillet from the bead ring up to the ceiling
CREST_R = 41.5      # sidewall crest radius (sidewall rises outward to here)
CREST_Z = 21.95     # sidewall crest height
SIDE_RAD = 50.0     # sidewall arc radius in the r-z profile (dished sidewall)
Z_TOOTH_OUT = 21.2  # shoulder teeth top at the outer radius
Z_TOOTH_IN = 21.8   # shoulder teeth top where they meet the sidewall
R_TOOTH_IN = 42.0   # inner end of the shoulder teeth
N_PITCH = 18        # tread pitches around the tire
PITCH = 360.0 / N_PITCH

# tread pattern, unwrapped (s = tangential mm on the -Y side, z = axial mm), upper half;
# the lower half is the same pattern turned 180 deg about the X axis
T_APEX = (3.62, 16.74)    # top lug: apex of the chevron
T_ARM_ANG = 40.0          # top lug: upper arm angle (runs up over the shoulder), deg
T_ARM_T = 3.0             # top lug: upper arm width
T_FOOT = ((-0.559, -0.829), 5.85, 3.0)  # top lug: foot direction, length, width
C_APEX = (-1.7, 8.9)      # middle chevron '>' outer apex
C_UP_TIP = (-9.3, 14.1)   # middle chevron upper arm outer tip (square end)
C_LO_TIP = ((-6.6, 1.85), (-10.0, 1.85))  # middle chevron lower arm flat end (outer, inner)
C_ARM_T = 2.7             # middle chevron upper arm width
LUG_B = [(0.54, 1.85), (4.59, 1.85), (6.87, 5.77), (3.94, 7.39)]  # small block

# letters (raised H / Y around both sidewalls)
R_LETTER = 34.6
LET_RAISE = 1.2     # letters stand proud of the sidewall by this much
H_H, H_W = 6.1, 5.4
Y_H, Y_W = 7.3, 6.7
LET_T = 1.25
ANG_TOP = (33.6, 13.6)   # (first H, first Y) on the top sidewall, deg; repeats every 40 deg
ANG_BOT = (6.4, 26.4)    # bottom sidewall, before the 180 deg flip about X (ends up at the same angles as the top)

SEAM_ANGLE = 83.6   # where the revolved surfaces close (tucked between two letters, out of the main view)

VIEW = {"azimuth": 45, "elevation": 26}

SH_RAD = R_C - CREST_R            # shoulder radius (tangent to crest and tread)
SH_Z = CREST_Z - SH_RAD           # height where shoulder meets tread cylinder
SIDE_CZ = CREST_Z - SIDE_RAD      # sidewall arc centre height (centre at r = CREST_R)


def side_z(r, off=0.0):
    return SIDE_CZ + math.sqrt((SIDE_RAD + off) ** 2 - (r - CREST_R) ** 2)


# ---------------- carcass (hollow, revolved profiles) ----------------
def _outer_solid():
    s_in = (SIDE_IN, side_z(SIDE_IN))
    smid_r = 0.5 * (SIDE_IN + CREST_R)
    smid = (smid_r, side_z(smid_r))
    a = math.radians(45)
    shmid = (CREST_R + SH_RAD * math.sin(a), SH_Z + SH_RAD * math.cos(a))

    def m(p):
        return (p[0], -p[1])

    wp = (
        cq.Workplane("XZ")
        .moveTo(0, -Z_BEAD)
        .lineTo(0, Z_BEAD)
        .lineTo(R_BEAD_FLAT, Z_BEAD)
        .threePointArc(LIP_MID, s_in)
        .threePointArc(smid, (CREST_R, CREST_Z))
        .threePointArc(shmid, (R_C, SH_Z))
        .lineTo(R_C, -SH_Z)
        .threePointArc(m(shmid), (CREST_R, -CREST_Z))
        .threePointArc(m(smid), m(s_in))
        .threePointArc(m(LIP_MID), (R_BEAD_FLAT, -Z_BEAD))
        .close()
    )
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


def _cavity_solid():
    """air cavity of the tire plus the through opening inside the beads"""
    ri = R_C - WALL
    c = CAV_CORNER
    f = BEAD_FILLET
    k = math.radians(45)

    def m(p):
        return (p[0], -p[1])

    # bead ring hangs below the flat cavity ceiling; fillet from bead to ceiling, small round at the tread
    b_out = (BEAD_OUT_R, Z_BEAD_IN)
    f_c = (BEAD_OUT_R + f, Z_BEAD_IN)
    f_mid = (f_c[0] - f * math.cos(k), f_c[1] + f * math.sin(k))
    f_end = (f_c[0], Z_BEAD_IN + f)                # = ceiling start
    corner_mid = (ri - c + c * math.cos(k), CEIL_Z - c + c * math.sin(k))
    zt = Z_BEAD + 5.0
    wp = (
        cq.Workplane("XZ")
        .moveTo(0, -zt)
        .lineTo(R_BORE, -zt)
        .lineTo(R_BORE, -Z_BEAD)
        .lineTo(R_BEAD_IN, -Z_BEAD_IN)
        .lineTo(*m(b_out))
        .threePointArc(m(f_mid), m(f_end))
        .lineTo(ri - c, -CEIL_Z)
        .threePointArc(m(corner_mid), (ri, -(CEIL_Z - c)))
        .lineTo(ri, CEIL_Z - c)
        .threePointArc(corner_mid, (ri - c, CEIL_Z))
        .lineTo(*f_end)
        .threePointArc(f_mid, b_out)
        .lineTo(R_BEAD_IN, Z_BEAD_IN)
        .lineTo(R_BORE, Z_BEAD)
        .lineTo(R_BORE, zt)
        .lineTo(0, zt)
        .close()
    )
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


def letter_envelope():
    """solid of revolution whose top follows the sidewall offset by LET_RAISE"""
    r0, r1 = R_LETTER - 5.0, min(R_LETTER + 5.0, CREST_R)
    mid = 0.5 * (r0 + r1)
    wp = (
        cq.Workplane("XZ")
        .moveTo(r0, 15.0)
        .lineTo(r0, side_z(r0, LET_RAISE))
        .threePointArc((mid, side_z(mid, LET_RAISE)), (r1, side_z(r1, LET_RAISE)))
        .lineTo(r1, 15.0)
        .close()
    )
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


def lug_clip():
    """outer envelope of the tread lugs: R_O cylinder capped by a shallow cone over the shoulder"""
    wp = (
        cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(R_O, 0)
        .lineTo(R_O, Z_TOOTH_OUT)
        .lineTo(R_TOOTH_IN, Z_TOOTH_IN)
        .lineTo(0, Z_TOOTH_IN)
        .close()
    )
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


# ---------------- helpers ----------------
def _unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def _line_x(p, d, q, e):
    """intersection of line p + l*d with line q + m*e"""
    det = d[0] * (-e[1]) - d[1] * (-e[0])
    rx, ry = q[0] - p[0], q[1] - p[1]
    l = (rx * (-e[1]) - ry * (-e[0])) / det
    return (p[0] + l * d[0], p[1] + l * d[1])


def thick_polyline(pts, t):
    """outline of a polyline with thickness t (mitred joins, square ends)"""
    n = len(pts)
    left, right = [], []
    for i in range(n):
        if i == 0 or i == n - 1:
            a, b = (pts[0], pts[1]) if i == 0 else (pts[i - 1], pts[i])
            d = _unit((b[0] - a[0], b[1] - a[1]))
            off = (-d[1] * t / 2, d[0] * t / 2)
        else:
            d0 = _unit((pts[i][0] - pts[i - 1][0], pts[i][1] - pts[i - 1][1]))
            d1 = _unit((pts[i + 1][0] - pts[i][0], pts[i + 1][1] - pts[i][1]))
            n0, n1 = (-d0[1], d0[0]), (-d1[1], d1[0])
            m = _unit((n0[0] + n1[0], n0[1] + n1[1]))
            k = (t / 2) / (m[0] * n0[0] + m[1] * n0[1])
            off = (m[0] * k, m[1] * k)
        left.append((pts[i][0] + off[0], pts[i][1] + off[1]))
        right.append((pts[i][0] - off[0], pts[i][1] - off[1]))
    return left + right[::-1]


# ---------------- tread lug outlines ----------------
# unwrapped tread coordinates (s = tangential mm, z = axial mm), upper half,
# for the pitch centred on the -Y side of the tire.
def lug_T():
    """top lug: long upper arm running over the shoulder + short foot"""
    apex = T_APEX
    du = _unit((-math.cos(math.radians(T_ARM_ANG)), math.sin(math.radians(T_ARM_ANG))))
    t_arm = T_ARM_T
    e = _unit(T_FOOT[0])                              # foot direction
    foot_len, t_foot = T_FOOT[1], T_FOOT[2]
    f_o = (apex[0] + foot_len * e[0], apex[1] + foot_len * e[1])
    nf = (e[1], -e[0])                                # normal of the foot, pointing up-left
    f_i = (f_o[0] + t_foot * nf[0], f_o[1] + t_foot * nf[1])
    nl = (du[1], -du[0]) if du[1] > 0 else (-du[1], du[0])  # down-left normal
    nl = (-abs(nl[0]), -abs(nl[1]))
    lo = (apex[0] + t_arm * nl[0], apex[1] + t_arm * nl[1])
    corner = _line_x(lo, du, f_i, e)
    zt = 27.0
    up_far = (apex[0] + (zt - apex[1]) / du[1] * du[0], zt)
    lo_far = (lo[0] + (zt - lo[1]) / du[1] * du[0], zt)
    return [f_o, apex, up_far, lo_far, corner, f_i]


def lug_C():
    """middle chevron '>' with perpendicular upper end and flat lower end"""
    a_o = C_APEX
    u_o = C_UP_TIP
    l_o, l_i = C_LO_TIP
    t_u = C_ARM_T
    d = _unit((u_o[0] - a_o[0], u_o[1] - a_o[1]))
    e = _unit((l_o[0] - a_o[0], l_o[1] - a_o[1]))
    u_i = (u_o[0] - t_u * d[1], u_o[1] + t_u * d[0])
    if u_i[1] > u_o[1]:
        u_i = (u_o[0] + t_u * d[1], u_o[1] - t_u * d[0])
    a_i = _line_x(u_i, d, l_i, e)
    return [a_o, u_o, u_i, a_i, l_i, l_o]


def radial_prism(poly, r_in, r_out):
    plane = cq.Plane(origin=(0, -r_in, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    return cq.Workplane(plane).polyline(poly).close().extrude(r_out - r_in)


def pitch_unit():
    t = radial_prism(lug_T(), R_TOOTH_IN, R_O + 2)
    c = radial_prism(lug_C(), R_C - 1.5, R_O + 2)
    b = radial_prism(LUG_B, R_C - 1.5, R_O + 2)
    unit = t.union(c).union(b)
    return unit.intersect(lug_clip()).val()


# ---------------- letters ----------------
def _let_solid(polys):
    s = None
    for p in polys:
        w = cq.Workplane("XY").workplane(offset=18.0).polyline(p).close().extrude(7.0)
        s = w if s is None else s.union(w)
    return s.val()


def _rect(cx, cy, w, h):
    return [(cx - w / 2, cy - h / 2), (cx + w / 2, cy - h / 2), (cx + w / 2, cy + h / 2), (cx - w / 2, cy + h / 2)]


def letter_H():
    w, h, t = H_W, H_H, LET_T
    return _let_solid([
        _rect(-w / 2 + t / 2, 0, t, h),
        _rect(w / 2 - t / 2, 0, t, h),
        _rect(0, 0, w - t, t),
    ])


def letter_Y():
    w, h, t = Y_W, Y_H, LET_T
    vj = 0.12 * h
    stem = _rect(0, (-h / 2 + vj) / 2, t, vj + h / 2)
    arm = thick_polyline([(-w / 2 + t / 2, h / 2 - t / 2), (0, vj), (w / 2 - t / 2, h / 2 - t / 2)], t)
    return _let_solid([stem, arm])


def build():
    body = _outer_solid().val().rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
    cavity = _cavity_solid().val().rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

    unit = pitch_unit()
    upper = [unit.rotate((0, 0, 0), (0, 0, 1), PITCH * k) for k in range(N_PITCH)]

    # letters on the top sidewall, alternating H / Y every 20 deg
    h = letter_H().translate((0, R_LETTER, 0))
    y = letter_Y().translate((0, R_LETTER, 0))
    env = letter_envelope().val()

    def letters(angs):
        lets = []
        for k in range(N_PITCH // 2):
            lets.append(h.rotate((0, 0, 0), (0, 0, 1), angs[0] + 40 * k - 90))
            lets.append(y.rotate((0, 0, 0), (0, 0, 1), angs[1] + 40 * k - 90))
        return env.intersect(cq.Compound.makeCompound(lets))

    lower_src = list(upper)
    upper.append(letters(ANG_TOP))
    lower_src.append(letters(ANG_BOT))

    # lower half: 180 deg rotation about X (point-symmetric tread, letters on both sides)
    lower = [s.rotate((0, 0, 0), (1, 0, 0), 180) for s in lower_src]

    res = body.fuse(*upper, *lower).cut(cavity).clean()
    solids = res.Solids()
    return cq.Workplane("XY").newObject(solids if len(solids) != 1 else [solids[0]])


result = build()
